import math
import cadquery as cq

# Two identical cup halves (coaxial on X) joined by a central hub and interleaved
# claw jaws, each with a fork of two bent arms and a 10-tooth pinion on a cross pin.  The -X half is the
# +X half turned 180 deg about the (0,1,-1) axis (X->-X, Y->-Z, Z->-Y).

# ---------------- driving dimensions (mm) ----------------
R = 25.0                  # outer radius of each cup
R_IN = 0.89 * R           # inner radius of the cup wall
X_BODY0 = 0.275 * R       # inner (closed) end of the cup body
X_BODY1 = 1.695 * R       # outer (open) end of the cup body
X_FLOOR = 0.45 * R        # inside face of the cup floor
LIP_R = 0.878 * R         # locating lip radius
X_LIP0 = 0.162 * R        # lip end face
HUB_R = 0.27 * R          # central hub joining the two cups

BAND_HALF = 30.0          # half angle of a latch band / jaw (deg)
BAND_X1 = 1.755 * R       # band extension past the rim
JAW_X0 = 0.06 * R         # jaw tip (toward the other half)
JAW_R0 = 0.55 * R         # jaw inner radius
JAW_HOLE_R = 0.035 * R
JAW_HOLE_RP = 0.80 * R    # pitch radius of the axial holes in the jaw ends
JAW_HOLE_DA = 15.0        # angular offset of those holes from the jaw centre

# latch ramps: (band edge deg, width deg (sign = side), depth at the rim end)
RAMPS = ((120.0, -12.0, 0.10 * R), (240.0, -24.0, 0.08 * R))
FACETED_BANDS = (90.0,)   # bands whose surface is two flat facets

KEY_A0, KEY_A1 = 167.0, 198.0   # raised key on the locating lip (deg)
KEY_R = 0.92 * R

PIN_HOLE_R = 0.034 * R    # small radial holes in the shell
BODY_HOLES_X = (0.50 * R, 1.32 * R)
BAND_HOLE_X = 0.42 * R

ARM_T = 0.11 * R          # fork arm plate thickness
ARM_W = 0.20 * R          # fork arm half width
ARM_X_IN = 0.75 * R       # where the arm starts inside the cup
ARM_X_BEND = 2.45 * R     # start of the straight tip
ARM_X_TIP = 2.79 * R      # arm tip
ARM_Y_TIP = 0.665 * R     # outer face of the straight tip
ARM_BEND1 = 0.25 * R      # centre-line bend radius at the rim
ARM_BEND2 = 0.40 * R      # centre-line bend radius near the tip
ARM_TIP_RND = 0.07 * R
ARM_HOLE_R = 0.040 * R
ARM_HOLE_X = 2.626 * R

GEAR_X = 1.36 * R         # pinion axis position
GEAR_RT = 0.406 * R       # tip radius
GEAR_RR = 0.27 * R        # root radius
GEAR_TIP_HA = 5.5         # half angle of a tooth tip land (deg)
GEAR_ROOT_HA = 9.5        # half angle of a tooth at the root (deg)
GEAR_TIP_FIL = 0.025 * R
GEAR_ROOT_FIL = 0.045 * R
GEAR_N = 10
GEAR_Y0 = -0.505 * R
GEAR_Y1 = 0.34 * R
PIN_R = 0.064 * R
PIN_Y0 = -0.80 * R
PIN_Y1 = 0.80 * R
PIN_END_R = 0.05 * R      # reduced journal at the pin ends
PIN_END_L = 0.035 * R


def sector(r0, r1, a0, a1, x0, x1):
    """Annular sector (angles in deg, measured from +Y toward +Z) extruded along X.
    Made as ring intersected with a planar wedge so its cylinders coincide exactly with
    the cup's own cylinders."""
    ring = cq.Workplane("YZ", origin=(x0, 0, 0)).circle(r1).circle(r0).extrude(x1 - x0)
    big = 3.0 * r1
    pts = [(0.0, 0.0)]
    n = 4
    for i in range(n + 1):
        a = math.radians(a0 + (a1 - a0) * i / n)
        pts.append((big * math.cos(a), big * math.sin(a)))
    wedge = (
        cq.Workplane("YZ", origin=(x0 - 1.0, 0, 0))
        .polyline(pts)
        .close()
        .extrude(x1 - x0 + 2.0)
    )
    return ring.intersect(wedge)


def _unit(v):
    L = math.hypot(v[0], v[1])
    return (v[0] / L, v[1] / L)


def offset_fillet_path(pts, d, rbs):
    """Offset an open polyline by d (left positive) and round its interior corners.
    rbs are centre-line bend radii.  Returns a list of ('L', p0, p1) / ('A', p0, pm, p1)."""
    n = len(pts)
    us = [_unit((pts[i + 1][0] - pts[i][0], pts[i + 1][1] - pts[i][1])) for i in range(n - 1)]
    ns = [(-u[1], u[0]) for u in us]
    cur = (pts[0][0] + d * ns[0][0], pts[0][1] + d * ns[0][1])
    prims = []
    for i in range(1, n - 1):
        u1, u2 = us[i - 1], us[i]
        n1, n2 = ns[i - 1], ns[i]
        cross = u1[0] * u2[1] - u1[1] * u2[0]
        dot = u1[0] * u2[0] + u1[1] * u2[1]
        th = math.atan2(cross, dot)
        s = 1.0 if th > 0 else -1.0
        # offset vertex = intersection of the two offset lines
        p = pts[i]
        a1 = (p[0] + d * n1[0], p[1] + d * n1[1])
        a2 = (p[0] + d * n2[0], p[1] + d * n2[1])
        # solve a1 + t u1 = a2 + q u2
        det = u1[0] * (-u2[1]) - u1[1] * (-u2[0])
        rx, ry = a2[0] - a1[0], a2[1] - a1[1]
        t = (rx * (-u2[1]) - ry * (-u2[0])) / det
        V = (a1[0] + t * u1[0], a1[1] + t * u1[1])
        r = rbs[i - 1] - d * s
        L = r * math.tan(abs(th) / 2)
        T1 = (V[0] - L * u1[0], V[1] - L * u1[1])
        T2 = (V[0] + L * u2[0], V[1] + L * u2[1])
        C = (T1[0] + s * r * n1[0], T1[1] + s * r * n1[1])
        w = _unit((V[0] - C[0], V[1] - C[1]))
        M = (C[0] + r * w[0], C[1] + r * w[1])
        prims.append(("L", cur, T1))
        prims.append(("A", T1, M, T2))
        cur = T2
    end = (pts[-1][0] + d * ns[-1][0], pts[-1][1] + d * ns[-1][1])
    prims.append(("L", cur, end))
    return prims


def make_arm(side):
    """Bent fork arm: plate normal to Y, at +Y (side=1) or -Y (side=-1)."""
    yc_in = R_IN - ARM_T / 2 + 0.004 * R
    yc_tip = ARM_Y_TIP - ARM_T / 2
    centre = [
        (ARM_X_IN, yc_in),
        (X_BODY1, yc_in),
        (ARM_X_BEND, yc_tip),
        (ARM_X_TIP + 0.3 * R, yc_tip),
    ]
    outer = offset_fillet_path(centre, ARM_T / 2, [ARM_BEND1, ARM_BEND2])
    inner = offset_fillet_path(centre, -ARM_T / 2, [ARM_BEND1, ARM_BEND2])
    wp = cq.Workplane("XY", origin=(0, 0, -ARM_W)).moveTo(*outer[0][1])
    for pr in outer:
        if pr[0] == "L":
            wp = wp.lineTo(*pr[2])
        else:
            wp = wp.threePointArc(pr[2], pr[3])
    wp = wp.lineTo(*inner[-1][2])
    for pr in reversed(inner):
        if pr[0] == "L":
            wp = wp.lineTo(*pr[1])
        else:
            wp = wp.threePointArc(pr[2], pr[1])
    plate = wp.close().extrude(2 * ARM_W)
    # side outline (XZ): long bar with rounded tip corners
    L = ARM_X_TIP - ARM_X_IN + 0.2 * R
    outline = (
        cq.Workplane("XZ", origin=(0, 2 * R, 0))
        .center(ARM_X_TIP - L / 2, 0)
        .rect(L, 2 * ARM_W)
        .extrude(4 * R)
        .edges("|Y and >X")
        .fillet(ARM_TIP_RND)
    )
    arm = plate.intersect(outline)
    hole = (
        cq.Workplane("XZ", origin=(0, 2 * R, 0))
        .center(ARM_HOLE_X, 0)
        .circle(ARM_HOLE_R)
        .extrude(4 * R)
    )
    arm = arm.cut(hole)
    if side < 0:
        arm = arm.mirror("XZ")
    return arm


def make_gear():
    """10-tooth pinion (axis along Y): straight-flank teeth, tip and root arcs."""
    pitch = 360.0 / GEAR_N

    def pol(r, a):
        a = math.radians(a)
        return (GEAR_X + r * math.cos(a), r * math.sin(a))

    # profile on an XZ workplane (local x = global X, local y = global Z), extruded toward -Y
    wp = cq.Workplane("XZ", origin=(0, GEAR_Y1, 0))
    c0 = 90.0
    wp = wp.moveTo(*pol(GEAR_RR, c0 - GEAR_ROOT_HA))
    for i in range(GEAR_N):
        c = c0 + i * pitch
        wp = wp.lineTo(*pol(GEAR_RT, c - GEAR_TIP_HA))
        wp = wp.threePointArc(pol(GEAR_RT, c), pol(GEAR_RT, c + GEAR_TIP_HA))
        wp = wp.lineTo(*pol(GEAR_RR, c + GEAR_ROOT_HA))
        wp = wp.threePointArc(pol(GEAR_RR, c + pitch / 2), pol(GEAR_RR, c + pitch - GEAR_ROOT_HA))
    gear = wp.close().extrude(GEAR_Y1 - GEAR_Y0)

    def _edges_at(radius_min, radius_max):
        sel = []
        for e in gear.edges("|Y").vals():
            c = e.Center()
            rr = math.hypot(c.x - GEAR_X, c.z)
            if radius_min <= rr <= radius_max:
                sel.append(e)
        return sel

    try:
        tips = _edges_at(0.5 * (GEAR_RT + GEAR_RR), 2 * GEAR_RT)
        gear = gear.newObject(tips).fillet(GEAR_TIP_FIL)
        roots = _edges_at(0.0, 0.5 * (GEAR_RT + GEAR_RR))
        gear = gear.newObject(roots).fillet(GEAR_ROOT_FIL)
    except Exception:
        pass
    pin = (
        cq.Workplane("XZ", origin=(GEAR_X, PIN_Y1 - PIN_END_L, 0))
        .circle(PIN_R)
        .extrude(PIN_Y1 - PIN_Y0 - 2 * PIN_END_L)
    )
    for y_end, length in ((PIN_Y1, PIN_END_L), (PIN_Y0 + PIN_END_L, PIN_END_L)):
        journal = (
            cq.Workplane("XZ", origin=(GEAR_X, y_end, 0))
            .circle(PIN_END_R)
            .extrude(length + 0.01)
        )
        pin = pin.union(journal)
    return gear.union(pin)


def radial_hole(x, ang_deg, r_hole, depth):
    """Blind hole drilled radially inward from the outer surface at (x, angle)."""
    a = math.radians(ang_deg)
    d = cq.Vector(0, math.cos(a), math.sin(a))
    start = d * (R + 1.0)
    c = cq.Solid.makeCylinder(r_hole, depth + 1.0, cq.Vector(x, start.y, start.z), -d)
    return cq.Workplane("XY").add(c)


def make_ramp_cut(edge, width, depth):
    """Latch ramp: a planar wedge removed beside a band edge.  It is `depth` deep at the
    band edge at the rim end, spans `width` degrees (sign gives the side) and vanishes at
    the jaw tip."""
    def pt(x, r, a):
        a = math.radians(a)
        return cq.Vector(x, r * math.cos(a), r * math.sin(a))

    p1 = pt(BAND_X1, R - depth, edge)
    p2 = pt(BAND_X1, R, edge + width)
    p3 = pt(JAW_X0, R, edge)
    n = (p2 - p1).cross(p3 - p1).normalized()
    mid = pt(0.5 * (BAND_X1 + JAW_X0), R, edge + width / 2)
    if n.dot(cq.Vector(0, mid.y, mid.z)) < 0:
        n = -n
    pl = cq.Plane(origin=p1, xDir=(p3 - p1).normalized(), normal=n)
    slab = cq.Workplane(pl).rect(8 * R, 8 * R).extrude(2 * R)
    a_lo, a_hi = sorted((edge, edge + width + math.copysign(10.0, width)))
    wedge = sector(0.5 * R, 1.2 * R, a_lo, a_hi, JAW_X0 - 0.2, BAND_X1 + 0.2)
    return slab.intersect(wedge)


def make_facet_cuts(ac):
    """The band surface is two flat facets (chords ac-30..ac and ac..ac+30) instead of
    the cylinder: remove the thin circular segments outside those chords."""
    cut = None
    for a1, a2 in ((ac - BAND_HALF, ac), (ac, ac + BAND_HALF)):
        def p(r, a):
            a = math.radians(a)
            return (r * math.cos(a), r * math.sin(a))

        seg = (
            cq.Workplane("YZ", origin=(JAW_X0 - 0.5, 0, 0))
            .polyline([p(R, a1), p(1.5 * R, a1), p(1.5 * R, a2), p(R, a2)])
            .close()
            .extrude(BAND_X1 - JAW_X0 + 1.0)
        )
        cut = seg if cut is None else cut.union(seg)
    return cut


def make_half():
    body = cq.Workplane("YZ", origin=(X_BODY0, 0, 0)).circle(R).extrude(X_BODY1 - X_BODY0)
    bore = cq.Workplane("YZ", origin=(X_FLOOR, 0, 0)).circle(R_IN).extrude(X_BODY1 - X_FLOOR + 1)
    body = body.cut(bore)
    lip = cq.Workplane("YZ", origin=(X_LIP0, 0, 0)).circle(LIP_R).extrude(X_BODY0 - X_LIP0 + 0.5)
    body = body.union(lip)
    for ac in (90.0, 270.0):
        # band extension beyond the rim
        ext = sector(R_IN, R, ac - BAND_HALF, ac + BAND_HALF, X_BODY1 - 0.5, BAND_X1)
        body = body.union(ext)
        # claw jaw reaching across the gap toward the other half
        jaw = sector(JAW_R0, R, ac - BAND_HALF, ac + BAND_HALF, JAW_X0, X_BODY0 + 0.5)
        body = body.union(jaw)
    key = sector(LIP_R - 0.5, KEY_R, KEY_A0, KEY_A1, X_LIP0, X_BODY0 + 0.5)
    body = body.union(key)
    body = body.union(make_arm(1)).union(make_arm(-1))
    # small holes
    cuts = None
    for ac in (90.0, 270.0):
        for da in (-JAW_HOLE_DA, JAW_HOLE_DA):
            a = math.radians(ac + da)
            h = (
                cq.Workplane("YZ", origin=(JAW_X0 - 1.0, 0, 0))
                .center(JAW_HOLE_RP * math.cos(a), JAW_HOLE_RP * math.sin(a))
                .circle(JAW_HOLE_R)
                .extrude(0.12 * R + 1.0)
            )
            cuts = h if cuts is None else cuts.union(h)
        cuts = cuts.union(radial_hole(BAND_HOLE_X, ac, PIN_HOLE_R, 0.12 * R))
    for ac in (0.0, 180.0):
        for hx in BODY_HOLES_X:
            cuts = cuts.union(radial_hole(hx, ac, PIN_HOLE_R, R - R_IN + 0.02 * R))
    body = body.cut(cuts)
    for ac in FACETED_BANDS:
        body = body.cut(make_facet_cuts(ac))
    for edge, width, depth in RAMPS:
        body = body.cut(make_ramp_cut(edge, width, depth))
    return body


half_a = make_half()
gear_a = make_gear()
hub = cq.Workplane("YZ", origin=(-X_LIP0 - 0.5, 0, 0)).circle(HUB_R).extrude(2 * X_LIP0 + 1.0)

half_b = half_a.rotate((0, 0, 0), (0, 1, -1), 180)
gear_b = gear_a.rotate((0, 0, 0), (0, 1, -1), 180)

result = half_a.union(hub).union(half_b).union(gear_a).union(gear_b)
